import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
A = 30.0            # half width of the square flange (flange = 2A x 2A)
FL_T = 3.0          # flange thickness
FL_R = 6.0          # flange corner radius
HOLE_OFF = 24.0     # mounting hole offset from centre (x and y)
HOLE_D = 6.2        # mounting hole diameter
H = 37.3            # overall height (body bottom to flange top)
WALL = 1.8          # body wall / floor thickness
Y_BACK = 18.0       # body is cut flat (and open) at this +Y position
BOT_R = 7.5         # outer bottom edge fillet radius
GROOVE_R = 6.2      # screw clearance groove radius (outside, at front holes)
BOSS_R = 7.6        # inner boss radius around the front screw grooves

R_OUT = A                 # body outline: half-circle radius at the front
R_IN = A - WALL           # cavity / flange opening radius
EXT = 20.0                # extra length used before the back cut
Z_FB = H - FL_T           # z of flange underside

FRONT_HOLES = [(-HOLE_OFF, -HOLE_OFF), (HOLE_OFF, -HOLE_OFF)]
ALL_HOLES = [(x, y) for x in (-HOLE_OFF, HOLE_OFF) for y in (-HOLE_OFF, HOLE_OFF)]


def d_shape(r, z0, z1, back):
    """Half-circle (front, -Y) plus rectangle to the back, extruded z0..z1."""
    circ = cq.Workplane("XY").workplane(offset=z0).circle(r).extrude(z1 - z0)
    rect = (cq.Workplane("XY").workplane(offset=z0)
            .center(0, back / 2.0).rect(2 * r, back).extrude(z1 - z0))
    return circ.union(rect)


# ---------------- outer body ----------------
outer = d_shape(R_OUT, 0.0, Z_FB, Y_BACK + EXT)
outer = outer.faces("<Z").edges().fillet(BOT_R)

# ---------------- inner cavity (with bosses left standing) ----------------
inner = d_shape(R_IN, WALL, Z_FB + 1.0, Y_BACK + EXT + 5.0)
inner = inner.faces("<Z").edges().fillet(BOT_R - WALL)
for (x, y) in FRONT_HOLES:
    boss = (cq.Workplane("XY").center(x, y).circle(BOSS_R)
            .extrude(H + 2.0).translate((0, 0, -1.0)))
    inner = inner.cut(boss)

body = outer.cut(inner)

# screw clearance grooves on the outside of the front corners
for (x, y) in FRONT_HOLES:
    groove = (cq.Workplane("XY").center(x, y).circle(GROOVE_R)
              .extrude(Z_FB + 1.0).translate((0, 0, -1.0)))
    body = body.cut(groove)

# open back: cut everything of the body beyond Y_BACK
back_cut = (cq.Workplane("XY").center(0, Y_BACK + 50.0)
            .rect(200.0, 100.0).extrude(Z_FB + 2.0).translate((0, 0, -1.0)))
body = body.cut(back_cut)

# ---------------- flange ----------------
flange = (cq.Workplane("XY").workplane(offset=Z_FB)
          .rect(2 * A, 2 * A).extrude(FL_T)
          .edges("|Z").fillet(FL_R))

part = body.union(flange)

# circular opening through the flange (notched by the front bosses)
opening = (cq.Workplane("XY").workplane(offset=Z_FB - 0.5)
           .circle(R_IN).extrude(FL_T + 1.0))
for (x, y) in FRONT_HOLES:
    b = (cq.Workplane("XY").workplane(offset=Z_FB - 1.0)
         .center(x, y).circle(BOSS_R).extrude(FL_T + 2.0))
    opening = opening.cut(b)
part = part.cut(opening)

# mounting holes
holes = (cq.Workplane("XY").workplane(offset=Z_FB - 1.0)
         .pushPoints(ALL_HOLES).circle(HOLE_D / 2.0).extrude(FL_T + 2.0))
part = part.cut(holes)

result = part

VIEW = {"azimuth": 45, "elevation": 26}
